import cadquery as cq

# Straight toy-train track section: two rails on three studded ties,
# lap-jointed rail ends with hollow tongues, coupling peg + socket at each end.
# The part is point symmetric (180 deg about Z); the -Y end is modelled and
# rotated to make the +Y end.

# ---------------- driving dimensions (mm) ----------------
P = 8.0             # stud pitch
W = 8 * P           # overall tie width (X)
L = 24 * P          # overall tie-to-tie length (Y)
T = 3.2             # tie (plate) thickness
STUD_R = 2.4
STUD_H = 1.8
RAIL_X = 20.0       # rail centre-line offset from part centre
FOOT_HW = 4.0       # half width of rail foot
FOOT_H = 3.5        # height of rail foot at its outer edge
SHOULDER_HW = 2.65  # rail shoulder (between foot and web)
SHOULDER_Z = 3.75
WEB_HW = 1.55       # half width of rail web at its base
WEB_Z = 4.55
HEAD_HW = 1.36      # half width of the rail crown
RAIL_H = 9.5        # rail height
END_FOOT_HW = 3.0   # end-segment (lap) flank half width at foot level
END_HEAD_Z = 7.6    # end-segment: vertical head sides above this height
END_TIE_D = 1 * P   # end tie depth (Y)
MID_TIE_D = 2 * P   # middle tie depth (Y)

TONGUE_L = 3.4      # end connector tongue projection beyond the tie
TONGUE_IN = 1.3     # tongue reaches this far past the rail centre line
TONGUE_OUT = 8.3    # and this far on the extended side
TONGUE_WALL = 0.85  # wall thickness of the hollow tongue
TONGUE_FLOOR = 1.2  # floor height inside the tongue recess
LAP_CUT = 7.6       # length of lapped rail end segment (from tongue end)

PEG_X = 8.0         # coupling peg / socket offset from centre line
PEG_R = 2.0
PEG_HOLE_R = 0.85
PEG_SLOT_HW = 2.7   # clearance notch around the peg
PEG_SLOT_D = 1.3
SOCKET_R = 2.25

GROUP_Y = [-64.0, -32.0, 32.0, 64.0]   # clip-pocket groups along each rail
POCKET_L = 7.3
POCKET_GAP = 1.6
POCKET_Z0 = 0.3
POCKET_Z1 = 3.2     # pockets stay closed at the top (ledge intact)
POCKET_D = 0.8
TAB_W = 1.8         # latch tabs standing in the pockets (flush with the foot face)
TAB_H = 2.3
TAB_R = 0.6         # rounded top corners of the tabs
TAB_FRAC = (0.3, 0.85)   # tab centres along a pocket (from its -Y end) on +X faces

CENTER_HOLE_R = 1.5
UNDER_DEPTH = 2.0   # depth of underside recesses
UNDER_WALL = 1.2
RAIL_CH_HW = 2.4    # half width of underside rail channel
RAIL_CH_H = 2.2


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def prism(pts, y0, y1):
    """closed XZ polygon extruded along +Y from y0 to y1"""
    return (cq.Workplane("XZ").polyline(pts).close().extrude(y1 - y0)
            .translate((0, y1, 0)))


def acc(a, b):
    return b if a is None else a.union(b)


def rail_profile(xc):
    half = [(FOOT_HW, 0), (FOOT_HW, FOOT_H), (SHOULDER_HW, SHOULDER_Z),
            (WEB_HW, WEB_Z), (HEAD_HW, RAIL_H)]
    right = [(xc + x, z) for (x, z) in half]
    left = [(xc - x, z) for (x, z) in reversed(half)]
    return right + left


def end_half_profile(xc, s):
    """lapped end segment: one half (s=-1: -X, s=+1: +X) of the rail head"""
    return [(xc, FOOT_H - 0.3), (xc + s * END_FOOT_HW, FOOT_H - 0.3),
            (xc + s * END_FOOT_HW, FOOT_H), (xc + s * HEAD_HW, END_HEAD_Z),
            (xc + s * HEAD_HW, RAIL_H), (xc, RAIL_H)]


# ---------------- ties ----------------
body = box(-W / 2, W / 2, -L / 2, -L / 2 + END_TIE_D, 0, T)
body = body.union(box(-W / 2, W / 2, L / 2 - END_TIE_D, L / 2, 0, T))
body = body.union(box(-W / 2, W / 2, -MID_TIE_D / 2, MID_TIE_D / 2, 0, T))

# ---------------- rails ----------------
for xc in (-RAIL_X, RAIL_X):
    body = body.union(prism(rail_profile(xc), -L / 2, L / 2))

# ---------------- studs ----------------
stud_x = [-28.0, -12.0, -4.0, 4.0, 12.0, 28.0]
stud_pts = []
for x in stud_x:
    for y in (-L / 2 + P / 2, L / 2 - P / 2, -P / 2, P / 2):
        stud_pts.append((x, y))
studs = (cq.Workplane("XY").workplane(offset=T).pushPoints(stud_pts)
         .circle(STUD_R).extrude(STUD_H))
body = body.union(studs)


# ---------------- rail end lap joints, tongues, coupling peg / socket ----------------
def end_features():
    """(add, cut) solids of the -Y end; the +Y end is the same turned 180 deg"""
    y_end = -L / 2
    y_tip = y_end - TONGUE_L
    add = None
    cut = None
    for xc in (-RAIL_X, RAIL_X):
        # rail head is replaced by a half-width lap segment over the end tie
        cut = acc(cut, box(xc - FOOT_HW - 0.5, xc + FOOT_HW + 0.5, y_tip - 1,
                           y_tip + LAP_CUT, FOOT_H, RAIL_H + 1))
        seg = prism(end_half_profile(xc, -1), y_tip, y_tip + LAP_CUT)
        # hollow tongue projecting past the tie
        tongue = box(xc - TONGUE_OUT, xc + TONGUE_IN, y_tip, y_end, 0, FOOT_H)
        recess = box(xc - TONGUE_OUT - 0.1, xc - END_FOOT_HW,
                     y_tip + TONGUE_WALL, y_end + 0.01, TONGUE_FLOOR, FOOT_H + 1)
        add = acc(add, tongue.cut(recess).union(seg))
    # coupling peg: hollow tube standing in a clearance notch of the tie edge
    cut = acc(cut, box(-PEG_X - PEG_SLOT_HW, -PEG_X + PEG_SLOT_HW, y_end - 1,
                       y_end + PEG_SLOT_D, -1, T + 1))
    peg = (cq.Workplane("XY").center(-PEG_X, y_end).circle(PEG_R)
           .circle(PEG_HOLE_R).extrude(T))
    bridge = box(-PEG_X - 0.9, -PEG_X + 0.9, y_end + PEG_R - 0.5,
                 y_end + PEG_SLOT_D + 0.3, 0, T)
    bridge = bridge.cut(cq.Workplane("XY").center(-PEG_X, y_end)
                        .circle(PEG_HOLE_R).extrude(T))
    add = add.union(peg).union(bridge)
    # socket for the neighbouring track's peg
    cut = cut.union(cq.Workplane("XY").center(PEG_X, y_end).circle(SOCKET_R)
                    .extrude(T + 2).translate((0, 0, -1)))
    return add, cut


e_add, e_cut = end_features()
body = body.cut(e_cut).cut(e_cut.rotate((0, 0, 0), (0, 0, 1), 180))
body = body.union(e_add).union(e_add.rotate((0, 0, 0), (0, 0, 1), 180))

# ---------------- clip pockets on both faces of each rail foot ----------------
pockets = None
tabs = None
for xc in (-RAIL_X, RAIL_X):
    for s in (-1, 1):
        xf = xc + s * FOOT_HW                     # foot face
        x0, x1 = sorted((xf, xf - s * POCKET_D))
        ex0 = x0 - (0.05 if s < 0 else 0)
        ex1 = x1 + (0.05 if s > 0 else 0)
        for gy in GROUP_Y:
            for k in (-1, 1):
                yc = gy + k * (POCKET_L + POCKET_GAP) / 2
                pockets = acc(pockets, box(ex0, ex1, yc - POCKET_L / 2, yc + POCKET_L / 2,
                                           POCKET_Z0, POCKET_Z1))
                for f in TAB_FRAC:
                    f = f if s > 0 else 1.0 - f       # point symmetry of the part
                    ty = yc - POCKET_L / 2 + f * POCKET_L
                    tb = (box(x0 - 0.02, x1 + 0.02, ty - TAB_W / 2, ty + TAB_W / 2,
                              POCKET_Z0 - 0.02, POCKET_Z0 + TAB_H)
                          .edges("|X and >Z").fillet(TAB_R))
                    tabs = acc(tabs, tb.intersect(box(x0, x1, ty - TAB_W, ty + TAB_W,
                                                      POCKET_Z0 - 0.02, POCKET_Z1)))
body = body.cut(pockets).union(tabs)

# ---------------- centre hole ----------------
body = body.cut(cq.Workplane("XY").circle(CENTER_HOLE_R).extrude(T + 2)
                .translate((0, 0, -1)))

# ---------------- underside recesses ----------------
under = None
wall = UNDER_WALL
inner_x0 = -RAIL_X + FOOT_HW + wall
inner_x1 = RAIL_X - FOOT_HW - wall
# middle tie, four cells between the rails
for (x0, x1) in ((inner_x0, -0.6), (0.6, inner_x1)):
    for (y0, y1) in ((-MID_TIE_D / 2 + wall, -0.6), (0.6, MID_TIE_D / 2 - wall)):
        under = acc(under, box(x0, x1, y0, y1, -0.1, UNDER_DEPTH))
# counterbore around the centre hole (hole passes only the thin top skin)
under = under.union(cq.Workplane("XY").circle(CENTER_HOLE_R + 0.9)
                    .extrude(UNDER_DEPTH + 0.1).translate((0, 0, -0.1)))
# outer plates of the middle tie and of the end ties
for sx in (-1, 1):
    xa, xb = sorted((sx * (RAIL_X + FOOT_HW + wall), sx * (W / 2 - wall)))
    under = acc(under, box(xa, xb, -MID_TIE_D / 2 + wall, MID_TIE_D / 2 - wall,
                           -0.1, UNDER_DEPTH))
    for sgn in (-1, 1):
        yc = sgn * (L / 2 - END_TIE_D / 2)
        under = acc(under, box(xa, xb, yc - END_TIE_D / 2 + wall, yc + END_TIE_D / 2 - wall,
                               -0.1, UNDER_DEPTH))
# rail channels between ribs
rib_y = [-L / 2 + END_TIE_D, -64.0, -32.0, -MID_TIE_D / 2,
         MID_TIE_D / 2, 32.0, 64.0, L / 2 - END_TIE_D]
for xc in (-RAIL_X, RAIL_X):
    for i in range(len(rib_y) - 1):
        y0, y1 = rib_y[i] + 0.8, rib_y[i + 1] - 0.8
        if y1 - y0 < 5:
            continue
        under = acc(under, box(xc - RAIL_CH_HW, xc + RAIL_CH_HW, y0, y1, -0.1, RAIL_CH_H))
body = body.cut(under)

result = body
